import math

import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 50.0          # overall width (X)
H = 114.0         # overall height (Z)
T_FRONT = 8.7     # front plate thickness (Y)
T_STEM = 9.05     # depth of the T-slot stem (Y)
T_HEAD = 10.25    # depth of the T-head (Y)
D = T_FRONT + T_STEM + T_HEAD   # overall depth

STEM_W = 8.1      # stem / web width (X)
HEAD_W = 22.1     # T-head width (X)
BASE_T = 9.0      # base plate thickness (Z)

TOP_SEC = 26.3    # height of upper wide section of front plate
BOT_SEC = 26.2    # height of lower wide section (above base)
FILLET_R = 5.2    # fillet at web / wide-section junction

HOLE_D = 5.3      # through hole
CB_D = 10.0       # counterbore (from the back of the front plate)
CB_DEPTH = 5.0
HOLE_X = 16.2     # hole offset from centre line

SCRIBE_W = 0.15   # fine scribe lines seen on the plate faces
SCRIBE_DEPTH = 0.15

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- derived ----------------
z_cut_lo = BASE_T + BOT_SEC
z_cut_hi = H - TOP_SEC

# front plate (y from 0 to T_FRONT), I-shaped in front view
front = cq.Workplane("XY").box(W, T_FRONT, H, centered=(True, False, False))
side_cut_w = W / 2 - STEM_W / 2
for sgn in (-1, 1):
    cx = sgn * (STEM_W / 2 + side_cut_w / 2)
    cutter = (
        cq.Workplane("XY")
        .box(side_cut_w, T_FRONT + 2, z_cut_hi - z_cut_lo,
             centered=(True, False, False))
        .translate((cx, -1, z_cut_lo))
    )
    front = front.cut(cutter)

# fillet the four concave corners (edges parallel to Y at the web)
for zc in (z_cut_lo, z_cut_hi):
    front = front.edges(
        cq.selectors.BoxSelector((-STEM_W / 2 - 0.1, -1, zc - 0.1),
                                 (STEM_W / 2 + 0.1, T_FRONT + 1, zc + 0.1))
    ).fillet(FILLET_R)

# stem and T-head (full height), base plate
stem = (cq.Workplane("XY").box(STEM_W, T_STEM, H, centered=(True, False, False))
        .translate((0, T_FRONT, 0)))
head = (cq.Workplane("XY").box(HEAD_W, T_HEAD, H, centered=(True, False, False))
        .translate((0, T_FRONT + T_STEM, 0)))
base = cq.Workplane("XY").box(W, D, BASE_T, centered=(True, False, False))

body = front.union(stem).union(head).union(base)

# counterbored mounting holes through the front plate (counterbore on the back)
z_top_hole = H - TOP_SEC / 2
z_bot_hole = BASE_T + BOT_SEC / 2
pts = [(-HOLE_X, z_top_hole), (HOLE_X, z_top_hole),
       (-HOLE_X, z_bot_hole), (HOLE_X, z_bot_hole)]

# workplane on the back face of the front plate, normal pointing -Y (into the plate)
back_wp = cq.Workplane(cq.Plane(origin=(0, T_FRONT, 0), xDir=(1, 0, 0), normal=(0, -1, 0)))
holes = back_wp.pushPoints(pts).circle(HOLE_D / 2).extrude(T_FRONT + 1)
cbores = back_wp.pushPoints(pts).circle(CB_D / 2).extrude(CB_DEPTH)
body = body.cut(holes).cut(cbores)


# ---------------- fine scribe lines ----------------
def scribe(p0, p1, y0, y1, ext0=0.0, ext1=0.0):
    """thin straight groove in the XZ plane from p0 to p1 (x, z), spanning y0..y1"""
    dx, dz = p1[0] - p0[0], p1[1] - p0[1]
    L = math.hypot(dx, dz)
    ux, uz = dx / L, dz / L
    sx, sz = p0[0] - ux * ext0, p0[1] - uz * ext0
    length = L + ext0 + ext1
    ang = math.degrees(math.atan2(dz, dx))
    return (
        cq.Workplane("XY")
        .box(length, y1 - y0, SCRIBE_W, centered=(False, False, True))
        .rotate((0, 0, 0), (0, 1, 0), -ang)
        .translate((sx, y0, sz))
    )


def on_circle(cx, cz, r, deg):
    a = math.radians(deg)
    return (cx + r * math.cos(a), cz + r * math.sin(a))


fil_cx = STEM_W / 2 + FILLET_R
fil_cz = z_cut_hi - FILLET_R

# front face, +X upper hole -> upper-right web fillet
s_front = scribe(on_circle(HOLE_X, z_top_hole, HOLE_D / 2, 195.0),
                 on_circle(fil_cx, fil_cz, FILLET_R, 130.0),
                 -1.0, SCRIBE_DEPTH, ext0=0.6, ext1=0.3)
# back face, -X upper counterbore -> upper-left web fillet (two lines, a "V")
s_back1 = scribe(on_circle(-HOLE_X, z_top_hole, CB_D / 2, -11.0),
                 on_circle(-fil_cx, fil_cz, FILLET_R, 0.0),
                 T_FRONT - SCRIBE_DEPTH, T_FRONT + 1.0, ext0=0.6, ext1=-0.15)
s_back2 = scribe(on_circle(-HOLE_X, z_top_hole, CB_D / 2, -52.0),
                 on_circle(-fil_cx, fil_cz, FILLET_R, 52.0),
                 T_FRONT - SCRIBE_DEPTH, T_FRONT + 1.0, ext0=0.6, ext1=0.3)
body = body.cut(s_front).cut(s_back1).cut(s_back2)

result = body
